import math
import cadquery as cq
from OCP.BRep import BRep_Tool
from OCP.BRepAdaptor import BRepAdaptor_Curve
from OCP.Geom import Geom_TrimmedCurve
from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge

# ---------------- driving dimensions (mm) ----------------
N_TEETH = 15           # number of gear teeth
MODULE = 2.0           # gear module
PRESSURE_ANGLE = 20.0  # deg
ADDENDUM = 1.0 * MODULE
DEDENDUM = 1.25 * MODULE
ROOT_FILLET = 0.5 * MODULE

GEAR_HEIGHT = 14.0     # gear height above the base plate
BASE_T = 6.0           # base plate thickness
BASE_R = 16.75         # radius of round part of base plate (concentric to gear)
TAB_CX = -20.0         # x of the centre of the tab's rounded end
TAB_R = BASE_R / 2.0   # radius of the tab's rounded end (tab spans y = -BASE_R .. 0)

BORE_D = 20.0          # blind bore in the top of the gear
BORE_DEPTH = 8.1
HOLE_D = 6.0           # small through hole at the centre

# ---------------- helpers ----------------
V = cq.Vector


def pol(r, a):
    return V(r * math.cos(a), r * math.sin(a), 0)


def merge_edges(edges, tol=1e-6):
    """Join a chain of (tangent) edges exactly into one B-spline edge."""
    comp = None
    for e in edges:
        ad = BRepAdaptor_Curve(e.wrapped)
        u0, u1 = ad.FirstParameter(), ad.LastParameter()
        crv = BRep_Tool.Curve_s(e.wrapped, u0, u1)
        tc = Geom_TrimmedCurve(crv, u0, u1)
        if comp is None:
            comp = GeomConvert_CompCurveToBSplineCurve(tc)
        else:
            if not comp.Add(tc, tol, True):
                raise ValueError("edges not connected")
    return cq.Edge(BRepBuilderAPI_MakeEdge(comp.BSplineCurve()).Edge())


def arc3(p0, p1, p2):
    return cq.Edge.makeThreePointArc(p0, p1, p2)


# ---------------- gear geometry ----------------
r_p = MODULE * N_TEETH / 2.0
r_a = r_p + ADDENDUM
r_f = r_p - DEDENDUM
alpha = math.radians(PRESSURE_ANGLE)
r_b = r_p * math.cos(alpha)
pitch_ang = 2 * math.pi / N_TEETH


def inv(a):
    return math.tan(a) - a


beta_b = math.pi / (2 * N_TEETH) + inv(alpha)   # half tooth angle on base circle
t_a = math.sqrt((r_a / r_b) ** 2 - 1.0)         # involute roll angle at tip
beta_a = beta_b - inv(math.atan(t_a))           # half tooth angle on tip circle


def involute(phi, side, n=5):
    """Involute flank of the tooth centred at angle phi.
    side=-1: flank on the clockwise side, side=+1: counter-clockwise side.
    Returns points (base -> tip) and unit tangents along that direction."""
    pts, tans = [], []
    rot = phi + side * beta_b
    for i in range(n):
        t = t_a * i / (n - 1)
        x = r_b * (math.cos(t) + t * math.sin(t))
        y = r_b * (math.sin(t) - t * math.cos(t))
        tx, ty = math.cos(t), math.sin(t)
        if side > 0:
            y, ty = -y, -ty
        c, s = math.cos(rot), math.sin(rot)
        pts.append(V(c * x - s * y, s * x + c * y, 0))
        tans.append(V(c * tx - s * ty, s * tx + c * ty, 0))
    return pts, tans


def fillet_pts(gamma, toward):
    """Root fillet between radial line at angle gamma and root circle.
    toward=+1: gap lies at larger angles. Returns (line_pt, mid_pt, root_pt, delta)."""
    rho = ROOT_FILLET
    d = r_f + rho
    delta = math.asin(rho / d)
    c = pol(d, gamma + toward * delta)
    a = pol(r_f, gamma + toward * delta)
    b = pol(d * math.cos(delta), gamma)
    vm = (a - c) + (b - c)
    m = c + vm.normalized() * rho
    return b, m, a, delta


def gap_edge(k):
    """One smooth edge: CCW flank of tooth k, root, CW flank of tooth k+1."""
    phi0 = k * pitch_ang
    phi1 = (k + 1) * pitch_ang
    edges = []
    # CCW-side flank of tooth k, from tip down to base circle
    p, t = involute(phi0, +1)
    p, t = p[::-1], [-v for v in t[::-1]]
    edges.append(cq.Edge.makeSpline(p, tangents=t))
    g0 = phi0 + beta_b
    b0, m0, a0, _ = fillet_pts(g0, +1)
    edges.append(cq.Edge.makeLine(p[-1], b0))
    edges.append(arc3(b0, m0, a0))
    g1 = phi1 - beta_b
    b1, m1, a1, _ = fillet_pts(g1, -1)
    edges.append(arc3(a0, pol(r_f, 0.5 * (phi0 + phi1)), a1))
    edges.append(arc3(a1, m1, b1))
    q, u = involute(phi1, -1)
    edges.append(cq.Edge.makeLine(b1, q[0]))
    edges.append(cq.Edge.makeSpline(q, tangents=u))
    return merge_edges(edges)


gear_edges = []
for k in range(N_TEETH):
    phi = k * pitch_ang
    gear_edges.append(arc3(pol(r_a, phi - beta_a), pol(r_a, phi), pol(r_a, phi + beta_a)))
    gear_edges.append(gap_edge(k))
gear_wire = cq.Wire.assembleEdges(gear_edges)
# ruled loft between the bottom and top outline = straight prism of the gear profile
gear = cq.Solid.makeLoft(
    [gear_wire.translate(V(0, 0, BASE_T)), gear_wire.translate(V(0, 0, BASE_T + GEAR_HEIGHT))],
    True,
)

# ---------------- base plate (one smooth side wall) ----------------
c45 = math.cos(math.radians(45))
base_edges = [
    cq.Edge.makeLine(V(-BASE_R, 0, 0), V(TAB_CX, 0, 0)),
    arc3(V(TAB_CX, 0, 0), V(TAB_CX - TAB_R, -TAB_R, 0), V(TAB_CX, -2 * TAB_R, 0)),
    cq.Edge.makeLine(V(TAB_CX, -2 * TAB_R, 0), V(0, -BASE_R, 0)),
    arc3(V(0, -BASE_R, 0), V(BASE_R * c45, BASE_R * c45, 0), V(-BASE_R, 0, 0)),
]
base_outline = merge_edges(base_edges)
base_wire = cq.Wire.assembleEdges([base_outline])
base = cq.Solid.makeLoft([base_wire, base_wire.translate(V(0, 0, BASE_T))], True)

body = cq.Workplane("XY").add(base).union(cq.Workplane("XY").add(gear))

# ---------------- bore and through hole ----------------
top_z = BASE_T + GEAR_HEIGHT
# (cylinder seam turned to 225 deg, away from the usual viewing directions)
bore = cq.Solid.makeCylinder(
    BORE_D / 2.0, BORE_DEPTH + 1.0, V(0, 0, top_z - BORE_DEPTH), V(0, 0, 1)
).rotate(V(0, 0, 0), V(0, 0, 1), 225)
hole = cq.Workplane("XY").workplane(offset=-1.0).circle(HOLE_D / 2.0).extrude(top_z + 2.0)

result = body.cut(bore).cut(hole)

VIEW = {"azimuth": 45, "elevation": 26}
